"""Spherical mounting bezel / cowl flange.

A flat mounting flange with a shallow spherical dome behind it.  The front
has a stepped recess that narrows with a 45-ish degree conical bore down to a
central opening at the crown of the dome.  Four bolt holes on a bolt circle
pass through the flange; behind each one a U-shaped screw-head clearance slot
(open towards the rim) is cut through the dome down to the flange back face.

Axis of revolution = +Y (flange front face at Y=0 faces the viewer in the
front view, the dome extends towards +Y).
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 100.0        # flange outer radius (OD 200)
T_FLANGE = 7.0       # flange thickness
L_TOTAL = 51.5       # overall axial length (flange front -> back edge of dome)
R_HOLE = 46.2        # central opening (bore) radius
L_BORE = 4.6         # length of the cylindrical bore at the back opening
R_REC = 82.0         # front recess radius
D_STEP = 11.0        # depth of the cylindrical step of the recess
R_BC = 93.0          # bolt circle radius
D_BOLT = 7.6         # bolt hole diameter
W_SLOT = 14.6        # width of the U-shaped screw-head clearance slot
N_BOLT = 4           # number of bolt holes (at 0/90/180/270 deg)

# ---------------- derived geometry ----------------
# Outer dome = sphere centred on the axis, passing through the flange rim
# (R_OUT, T_FLANGE) and the back edge of the opening (R_HOLE, L_TOTAL).
a0 = (L_TOTAL**2 + R_HOLE**2 - T_FLANGE**2 - R_OUT**2) / (2.0 * (L_TOTAL - T_FLANGE))
RS = math.hypot(T_FLANGE - a0, R_OUT)


def sphere_pt(r):
    """point (radius, axial) on the outer sphere at radius r"""
    return (r, a0 + math.sqrt(RS**2 - r**2))


mid = sphere_pt(0.5 * (R_OUT + R_HOLE))

# ---------------- body of revolution ----------------
# half cross-section in the XY plane (x = radius, y = axial), revolved about Y
prof = (
    cq.Workplane("XY")
    .moveTo(R_HOLE, L_TOTAL)
    .threePointArc(mid, (R_OUT, T_FLANGE))      # spherical dome
    .lineTo(R_OUT, 0.0)                         # flange rim
    .lineTo(R_REC, 0.0)                         # flange front face
    .lineTo(R_REC, D_STEP)                      # recess step wall
    .lineTo(R_HOLE, L_TOTAL - L_BORE)           # conical inner surface
    .close()                                    # short bore
)
body = prof.revolve(360.0, (0, 0, 0), (0, 1, 0))

# ---------------- bolt hole + clearance slot (one set, at +X) ----------------
# Workplane "XZ" has its normal along -Y, so a negative extrude goes to +Y.
rc = W_SLOT / 2.0
reach = L_TOTAL + 10.0

bolt_hole = (
    cq.Workplane("XZ", origin=(0, -5.0, 0))
    .center(R_BC, 0)
    .circle(D_BOLT / 2.0)
    .extrude(-(reach + 5.0))
)
# U-slot: half round end on the bolt axis, straight sides running out past the rim;
# it starts at the flange back face and runs through the whole dome.
slot = (
    cq.Workplane("XZ", origin=(0, T_FLANGE, 0))
    .moveTo(R_BC, -rc)
    .lineTo(R_OUT + 10.0, -rc)
    .lineTo(R_OUT + 10.0, rc)
    .lineTo(R_BC, rc)
    .threePointArc((R_BC - rc, 0.0), (R_BC, -rc))
    .close()
    .extrude(-reach)
)
cutter = bolt_hole.union(slot)

# polar pattern of the cutter about the part axis
for i in range(N_BOLT):
    body = body.cut(cutter.rotate((0, 0, 0), (0, 1, 0), 360.0 * i / N_BOLT))

result = body
VIEW = {"azimuth": 45, "elevation": 26}
